import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 60.0            # cap outer diameter
H = 10.2            # cap height (disc, without the boss)
TOP_FILLET = 2.3    # rounding of the top outer edge

RIM_W = 1.25        # flat bottom face of the outer skirt
GROOVE_W = 1.25     # radial width of the V-groove in the skirt bottom
GROOVE_D = 2.5      # depth of that groove (at its outer, vertical flank)
LIP_W = 1.2         # flat bottom face of the inner lip
FLOOR_Z = 6.5       # height of the cavity floor above the skirt face
WALL_FILLET = 5.5   # large fillet floor -> skirt inner wall

BOSS = 25.3         # square boss side
BOSS_R = 4.6        # boss vertical corner radius
BOSS_DROP = 7.05    # boss protrusion below the skirt face
BOSS_FILLET = 2.0   # boss to floor fillet

SOCKET = 19.5       # square socket side
SOCKET_R = 4.3      # socket corner radius
SOCKET_DEPTH = 14.8 # socket depth measured from the boss face
SOCKET_FILLET = 0.4 # small socket bottom fillet

SEAM_ANGLE = 100.0  # put revolve seams where the main views do not see them

R = D / 2.0
r1 = R - RIM_W          # skirt inner edge / groove outer flank
r2 = r1 - GROOVE_W      # groove inner edge / lip outer edge
r3 = r2 - LIP_W         # cavity wall radius


def revolve_profile(pts_builder):
    return pts_builder.revolve(360, (0, 0, 0), (0, 1, 0))


# ---------------- outer body (revolved) ----------------
outer = revolve_profile(
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R, 0)
    .lineTo(R, H - TOP_FILLET)
    .radiusArc((R - TOP_FILLET, H), -TOP_FILLET)
    .lineTo(0, H)
    .close()
)

# ---------------- underside cavity ----------------
cavity = revolve_profile(
    cq.Workplane("XZ")
    .moveTo(0, -1.0)
    .lineTo(r3, -1.0)
    .lineTo(r3, FLOOR_Z - WALL_FILLET)
    .radiusArc((r3 - WALL_FILLET, FLOOR_Z), -WALL_FILLET)
    .lineTo(0, FLOOR_Z)
    .close()
)

# V-groove between the outer skirt and the inner lip
groove = revolve_profile(
    cq.Workplane("XZ")
    .moveTo(r2 - 0.3, -0.3)
    .lineTo(r1, -0.3)
    .lineTo(r1, GROOVE_D)
    .lineTo(r2, 0)
    .close()
)

body = outer.cut(cavity).cut(groove)
body = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)

# ---------------- square boss ----------------
boss = (
    cq.Workplane("XY")
    .workplane(offset=-BOSS_DROP)
    .rect(BOSS, BOSS)
    .extrude(BOSS_DROP + FLOOR_Z + 0.5)
    .edges("|Z")
    .fillet(BOSS_R)
)
body = body.union(boss)

# fillet where the boss meets the cavity floor
half = BOSS / 2.0 + 0.5
body = body.edges(
    cq.selectors.BoxSelector((-half, -half, FLOOR_Z - 0.1), (half, half, FLOOR_Z + 0.1))
).fillet(BOSS_FILLET)

# ---------------- square socket in the boss ----------------
socket = (
    cq.Workplane("XY")
    .workplane(offset=-BOSS_DROP - 1.0)
    .rect(SOCKET, SOCKET)
    .extrude(SOCKET_DEPTH + 1.0)
    .edges("|Z")
    .fillet(SOCKET_R)
    .faces(">Z")
    .edges()
    .fillet(SOCKET_FILLET)
)
body = body.cut(socket)

result = body
